import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# axes: X = across the clevis, Y = motor axis (front face at Y=0, bracket toward +Y), Z = up
MOTOR_R = 50.0          # motor can radius
MOTOR_L = 37.0          # motor can length
HUB_R = 14.85           # front boss
HUB_GROOVE_R = 16.7
HUB_L = 3.5
SHAFT_R = 8.4
SHAFT_L = 1.9
FLANGE_R = 60.0
FLANGE_Y0, FLANGE_Y1 = 37.0, 50.5
FLANGE_HOLE_PCD_R = 55.3
FRONT_PLATE_Y0, FRONT_PLATE_Y1 = 50.5, 67.5   # bracket front (ring) plate
BRK_W = 47.0            # half width of the bracket
EAR_IN = 30.0           # inner face of the front ears
POCKET_HW = 37.0        # half width of the top pocket
TOP_Z = 117.4           # top of the bracket
PIN_Z = 100.7           # pivot axis height
FRONT_HOLE_Y = 33.75
FRONT_HOLE_R = 7.5
BACK_PIN_Y = 94.0
PIN_HEAD_R, PIN_HEAD_OUT = 10.7, 4.6
PIN_R, PIN_COLLAR_R, PIN_TIP_X = 5.1, 8.0, 18.5
BRIDGE_Y0, BRIDGE_Y1 = 62.0, 69.0
STEP_Z = 67.5           # top of the front plate between the ears
BACK_Y0, BACK_Y1 = 119.5, 136.3   # back plate
BACK_BOTTOM_R = 38.5
ARCH_Y0, ARCH_Y1, ARCH_TOP, ARCH_R = 67.5, 119.5, 66.4, 11.0
EAR_FILLET_R = 12.0      # ear inner face -> bridge face blend
FRONT_BLEND_R = 22.0     # concave blend side plate -> ring plate
CHAMF_Y, CHAMF_Z = 100.5, 81.6   # 45 deg chamfer at the top back
BACK_TAPER_Z = 49.0      # back plate sides start tapering here
BACK_CIRC_Z = 4.0        # centre of the round bottom of the back plate

Y_AX = cq.Vector(0, 1, 0)


def cyl_y(r, y0, y1, x=0.0, z=0.0):
    # seam turned to the lower left so it stays out of the main views
    c = cq.Solid.makeCylinder(r, y1 - y0, cq.Vector(x, y0, z), Y_AX)
    c = c.rotate(cq.Vector(x, y0, z), cq.Vector(x, y1, z), 225)
    return cq.Workplane("XY").add(c)


def cyl_x(r, x0, x1, y, z):
    return cq.Workplane("XY").add(
        cq.Solid.makeCylinder(r, x1 - x0, cq.Vector(x0, y, z), cq.Vector(1, 0, 0)))


def box(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


def rounded_wire(wp, pts, radii):
    """closed polygon with filleted corners (convex or concave) drawn on wp"""
    n = len(pts)
    corners = []
    for i in range(n):
        px, py = pts[i]
        r = radii[i]
        if r <= 0:
            corners.append(((px, py), (px, py), None))
            continue
        ax, ay = pts[i - 1]
        bx, by = pts[(i + 1) % n]
        d1 = (ax - px, ay - py)
        d2 = (bx - px, by - py)
        l1 = math.hypot(*d1)
        l2 = math.hypot(*d2)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (d2[0] / l2, d2[1] / l2)
        cosang = max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1]))
        ang = math.acos(cosang)
        t = r / math.tan(ang / 2)
        a = (px + d1[0] * t, py + d1[1] * t)
        b = (px + d2[0] * t, py + d2[1] * t)
        bis = (d1[0] + d2[0], d1[1] + d2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        dc = r / math.sin(ang / 2)
        c = (px + bis[0] * dc, py + bis[1] * dc)
        m = (c[0] - bis[0] * r, c[1] - bis[1] * r)
        corners.append((a, b, m))
    w = wp.moveTo(*corners[0][1])
    for i in range(1, n + 1):
        a, b, m = corners[i % n]
        w = w.lineTo(*a)
        if m is not None:
            w = w.threePointArc(m, b)
    return w.close()


# ---------------- motor can ----------------
motor = cyl_y(MOTOR_R, 0, MOTOR_L)
# front hub boss (chamfered) rising out of a shallow ring groove, and the shaft stub
hub = cyl_y(HUB_R, -HUB_L, 1.5).faces("<Y").edges().chamfer(1.6)
motor = motor.cut(cyl_y(HUB_GROOVE_R, -1, 1.0))
motor = motor.union(hub)
motor = motor.union(cyl_y(SHAFT_R, -HUB_L - SHAFT_L, -HUB_L + 0.5))
# two vertical slots left / right
for sx in (-1, 1):
    slot = (cq.Workplane("XZ", origin=(sx * 42.7, 0, 0)).slot2D(12.75, 4.35, angle=90)
            .extrude(-2.0))
    motor = motor.cut(slot)
# four small screw holes near the rim
for a in (60, 120, 240, 300):
    motor = motor.cut(cyl_y(1.0, -1, 4, 47.3 * math.cos(math.radians(a)),
                            47.3 * math.sin(math.radians(a))))
# rectangular cable window low on the face: its ceiling ramps down into the can
WIN_W, WIN_Z0, WIN_Z1, WIN_DEPTH = 26.0, -44.9, -25.9, 10.0
win = (cq.Workplane("XZ", origin=(0, 0, (WIN_Z0 + WIN_Z1) / 2)).rect(WIN_W, WIN_Z1 - WIN_Z0)
       .extrude(-(WIN_DEPTH + 3)).edges("|Y").fillet(3.0)).translate((0, -1, 0))
z_lo = WIN_Z0 - 5.0
y_lo = WIN_DEPTH * (WIN_Z1 - z_lo) / (WIN_Z1 - WIN_Z0)
ramp = (cq.Workplane("YZ", origin=(-20, 0, 0))
        .polyline([(-1.0, WIN_Z1 + 1.0 * (WIN_Z1 - WIN_Z0) / WIN_DEPTH), (-1.0, z_lo), (y_lo, z_lo)]).close()
        .extrude(40))
motor = motor.cut(win.intersect(ramp))

# ---------------- output flange ----------------
flange = cyl_y(FLANGE_R, FLANGE_Y0, FLANGE_Y1)
for k in range(6):
    a = math.radians(60 * k)
    flange = flange.cut(cyl_y(2.0, FLANGE_Y0 - 1, FLANGE_Y1 + 1,
                              FLANGE_HOLE_PCD_R * math.cos(a), FLANGE_HOLE_PCD_R * math.sin(a)))

# ---------------- bracket ----------------
# front ring plate: round at the bottom, blending with concave fillets into the
# flat outer faces of the side plates
def front_plate_solid():
    rf = FRONT_BLEND_R
    cx = BRK_W + rf
    zc = math.sqrt((FLANGE_R + rf) ** 2 - cx ** 2)
    tl = (BRK_W, zc)                                   # tangent point on side face
    k = FLANGE_R / (FLANGE_R + rf)
    tc = (cx * k, zc * k)                              # tangent point on ring
    u1 = ((tl[0] - cx) / rf, (tl[1] - zc) / rf)
    u2 = ((tc[0] - cx) / rf, (tc[1] - zc) / rf)
    um = (u1[0] + u2[0], u1[1] + u2[1])
    lm = math.hypot(*um)
    mid = (cx + rf * um[0] / lm, zc + rf * um[1] / lm)
    wp = cq.Workplane("XZ", origin=(0, FRONT_PLATE_Y0, 0))
    w = (wp.moveTo(-BRK_W, STEP_Z).lineTo(-BRK_W, zc)
         .threePointArc((-mid[0], mid[1]), (-tc[0], tc[1]))
         .threePointArc((0, -FLANGE_R), tc)
         .threePointArc(mid, tl)
         .lineTo(BRK_W, STEP_Z).close())
    return w.extrude(-(FRONT_PLATE_Y1 - FRONT_PLATE_Y0))


front_plate = front_plate_solid()

# side plate profile in the YZ plane (local x = Y, local y = Z)
side_pts = [
    (FRONT_PLATE_Y0, 50.0),
    (FRONT_PLATE_Y0, 75.45),  # concave blend into ear underside
    (19.4, 84.7),             # ear lower front corner
    (19.4, TOP_Z),            # ear top front corner (large round about the pivot)
    (CHAMF_Y, TOP_Z),         # start of the 45 deg top-back chamfer
    (BACK_Y1, CHAMF_Z),       # end of the chamfer on the back face
    (BACK_Y1, 60.0),
    (BACK_Y0, 55.0),
]
side_r = [0, 14.0, 18.5, 17.0, 11.0, 30.0, 0, 0]


def side_plate(x0, x1):
    wp = cq.Workplane("YZ", origin=(x0, 0, 0))
    return rounded_wire(wp, side_pts, side_r).extrude(x1 - x0)


sides = side_plate(EAR_IN, BRK_W).union(side_plate(-BRK_W, -EAR_IN))

bridge = box(-BRK_W, BRK_W, BRIDGE_Y0, BRIDGE_Y1, 55.0, TOP_Z)

# back plate: straight sides, tapering into a round bottom about the motor axis
def back_plate_solid():
    cz, R = BACK_CIRC_Z, BACK_BOTTOM_R
    dx, dz = BRK_W, BACK_TAPER_Z - cz
    d = math.hypot(dx, dz)
    phi = math.atan2(dz, dx)
    beta = math.acos(R / d)
    t = phi - beta
    tR = (R * math.cos(t), cz + R * math.sin(t))
    wp = cq.Workplane("XZ", origin=(0, BACK_Y0, 0))
    w = (wp.moveTo(-BRK_W, TOP_Z).lineTo(BRK_W, TOP_Z).lineTo(BRK_W, BACK_TAPER_Z)
         .lineTo(*tR).threePointArc((0, cz - R), (-tR[0], tR[1]))
         .lineTo(-BRK_W, BACK_TAPER_Z).close())
    return w.extrude(-(BACK_Y1 - BACK_Y0))


back = back_plate_solid()

bracket = front_plate.union(sides).union(bridge).union(back)
for k in range(6):
    a = math.radians(60 * k)
    bracket = bracket.cut(cyl_y(2.0, FRONT_PLATE_Y0 - 1, FRONT_PLATE_Y1 + 1,
                                FLANGE_HOLE_PCD_R * math.cos(a), FLANGE_HOLE_PCD_R * math.sin(a)))

# large concave fillets where the ear inner faces meet the bridge front face
for sx in (-1, 1):
    xe = sx * EAR_IN
    xc = xe - sx * EAR_FILLET_R
    fil = box(min(xe, xc), max(xe, xc), BRIDGE_Y0 - EAR_FILLET_R, BRIDGE_Y0, STEP_Z, TOP_Z)
    fil = fil.cut(cq.Workplane("XY").add(cq.Solid.makeCylinder(
        EAR_FILLET_R, TOP_Z - STEP_Z + 2, cq.Vector(xc, BRIDGE_Y0 - EAR_FILLET_R, STEP_Z - 1), cq.Vector(0, 0, 1))))
    bracket = bracket.union(fil)

# top-back 45 deg chamfer with rounded ends
cham = rounded_wire(cq.Workplane("YZ", origin=(-60, 0, 0)),
                    [(60.0, 200.0), (60.0, TOP_Z), (CHAMF_Y, TOP_Z), (BACK_Y1, CHAMF_Z),
                     (BACK_Y1, -60.0), (170.0, -60.0), (170.0, 200.0)],
                    [0, 0, 11.0, 30.0, 0, 0, 0])
bracket = bracket.cut(cham.extrude(120))


# arch opening through the side plates (open at the bottom)
arch = rounded_wire(cq.Workplane("YZ", origin=(-60, 0, 0)),
                    [(ARCH_Y0, -80), (ARCH_Y1, -80), (ARCH_Y1, ARCH_TOP), (ARCH_Y0, ARCH_TOP)],
                    [0, 0, ARCH_R, ARCH_R]).extrude(120)
bracket = bracket.cut(arch)

# top pocket between the side walls
pocket = (box(-POCKET_HW, POCKET_HW, BRIDGE_Y1, BACK_Y0, 40, 140).edges("|Z").fillet(6.0))
bracket = bracket.cut(pocket)

# front pivot holes through both ears with a keyway
bracket = bracket.cut(cyl_x(FRONT_HOLE_R, -BRK_W - 1, BRK_W + 1, FRONT_HOLE_Y, PIN_Z))
# keyway in the left ear only
bracket = bracket.cut(box(-BRK_W - 1, -EAR_IN + 1, FRONT_HOLE_Y - 1.5, FRONT_HOLE_Y + 1.5,
                          PIN_Z, PIN_Z + FRONT_HOLE_R + 2.0))

# vertical lubrication / set-screw hole through the left ear
bracket = bracket.cut(cq.Workplane("XY").add(cq.Solid.makeCylinder(
    1.5, 60, cq.Vector(-38.0, 33.0, 70.0), cq.Vector(0, 0, 1))))


# small counterbored cross hole through both side plates, and two small holes in the bridge
bracket = bracket.cut(cyl_x(1.65, -60, 60, 58.9, PIN_Z))
for sx in (-1, 1):
    xo = sx * BRK_W
    bracket = bracket.cut(cyl_x(3.75, xo - 1.5, xo + 1.5, 58.9, PIN_Z))
    bracket = bracket.cut(cyl_y(1.5, BRIDGE_Y0 - EAR_FILLET_R, BRIDGE_Y1 + 1, sx * 28.0, 100.0))

# triangular lightening pockets on the back face
tri_depth = 6.0
tris = [
    [(-35.0, 81.0), (35.0, 81.0), (0.0, 35.0)],
    [(42.0, 79.0), (36.0, 12.0), (10.0, 37.0)],
    [(-42.0, 79.0), (-10.0, 37.0), (-36.0, 12.0)],
]
for t in tris:
    tri = rounded_wire(cq.Workplane("XZ", origin=(0, BACK_Y1 + 1, 0)), t, [2.5, 2.5, 2.5]).extrude(tri_depth + 1)
    bracket = bracket.cut(tri)

# ---------------- pivot pins (slotted heads outside, stepped ends inside the pocket) ----------------
# counterbores for the slotted heads
for sx in (-1, 1):
    xo = sx * BRK_W
    bracket = bracket.cut(cyl_x(13.5, min(xo, xo - sx * 1.2), max(xo, xo - sx * 1.2), BACK_PIN_Y, PIN_Z))

for sx in (-1, 1):
    xi = sx * POCKET_HW
    bracket = bracket.cut(cyl_x(PIN_COLLAR_R + 1.5, min(xi, xi + sx * 1.0), max(xi, xi + sx * 1.0),
                                BACK_PIN_Y, PIN_Z))

pins = None
for sx, slot_ang in ((1, 27.0), (-1, -85.0)):
    xo = sx * BRK_W
    xb = xo - sx * 1.2                       # bottom of the counterbore
    xh = xo + sx * PIN_HEAD_OUT              # outer face of the head
    head = cyl_x(PIN_HEAD_R, min(xb, xh), max(xb, xh), BACK_PIN_Y, PIN_Z)
    head = head.faces(">X" if sx > 0 else "<X").edges().fillet(2.0)
    xs0, xs1 = xh - sx * 2.0, xh + sx * 3.0
    slot_cut = box(min(xs0, xs1), max(xs0, xs1), BACK_PIN_Y - 1.2, BACK_PIN_Y + 1.2, PIN_Z - 13, PIN_Z + 13)
    slot_cut = slot_cut.rotate((0, BACK_PIN_Y, PIN_Z), (1, BACK_PIN_Y, PIN_Z), slot_ang)
    head = head.cut(slot_cut)
    xi = sx * POCKET_HW
    xt = sx * PIN_TIP_X
    shank = cyl_x(PIN_R, min(xo, xt), max(xo, xt), BACK_PIN_Y, PIN_Z)
    shank = shank.faces("<X" if sx > 0 else ">X").edges().chamfer(0.8)
    collar = cyl_x(PIN_COLLAR_R, min(xi + sx * 1.0, xi - sx * 4.5), max(xi + sx * 1.0, xi - sx * 4.5),
                   BACK_PIN_Y, PIN_Z)
    p = head.union(shank).union(collar)
    pins = p if pins is None else pins.union(p)

# ---------------- internal drive parts seen through the side windows ----------------
drive = cyl_y(40.0, FRONT_PLATE_Y1 - 0.5, 70.5)
for k in range(6):
    a = math.radians(30 + 60 * k)
    drive = drive.cut(cyl_y(1.8, 68.5, 71, 35.5 * math.cos(a), 35.5 * math.sin(a)))
drive = drive.union(cyl_y(32.0, 70.0, 72.8))
drive = drive.union(cyl_y(29.0, 72.5, 93.5))
coupling = cyl_y(46.0, 91.8, 111.75)
coupling = coupling.cut(cyl_y(47, 102.5, 103.5).cut(cyl_y(45.2, 102.5, 103.5)))
for k in range(12):
    a = math.radians(15 + 30 * k)
    coupling = coupling.cut(cyl_y(2.3, 90, 95, 41.5 * math.cos(a), 41.5 * math.sin(a)))
coupling = coupling.cut(cyl_y(36.0, 90, 92.8))
drive = drive.union(coupling)
drive = drive.union(cyl_y(37.5, 111.5, BACK_Y0 + 0.5))
for k in range(8):
    a = math.radians(22.5 + 45 * k)
    drive = drive.union(cyl_y(3.0, 111.5, 116.5, 40.5 * math.cos(a), 40.5 * math.sin(a)))

# ---------------- rear connector (castellated ring around a pin face) ----------------
CONN_R_OUT, CONN_R_IN = 27.0, 21.0
CONN_TOP = BACK_Y1 + 6.2
conn = cyl_y(CONN_R_OUT, BACK_Y1 - 0.5, BACK_Y1 + 1.8)
crown = cyl_y(CONN_R_OUT - 1.0, BACK_Y1 + 1.5, CONN_TOP).cut(cyl_y(CONN_R_IN, BACK_Y1, CONN_TOP + 1))
for k in range(6):
    a = 60 * k
    notch = box(15, 30, BACK_Y1 + 1.8, CONN_TOP + 1, -4.0, 4.0).rotate((0, 0, 0), (0, 1, 0), -a)
    crown = crown.cut(notch)
conn = conn.union(crown)
# contact face with a ring of pin holes and a centre bore
conn = conn.cut(cyl_y(4.5, BACK_Y1 - 6.0, BACK_Y1 + 3))
for k in range(10):
    a = math.radians(18 + 36 * k)
    conn = conn.cut(cyl_y(2.6, BACK_Y1 - 5.0, BACK_Y1 + 3, 13.5 * math.cos(a), 13.5 * math.sin(a)))
bracket = bracket.cut(cyl_y(4.5, BACK_Y1 - 6.0, BACK_Y1 + 1))
for k in range(10):
    a = math.radians(18 + 36 * k)
    bracket = bracket.cut(cyl_y(2.6, BACK_Y1 - 5.0, BACK_Y1 + 1, 13.5 * math.cos(a), 13.5 * math.sin(a)))

result = (motor.union(flange).union(bracket).union(pins).union(drive).union(conn))

VIEW = {"azimuth": 45, "elevation": 26}
